import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 50.0          # overall width (X)
H = 85.0          # overall height (Z)
T_UP = 9.6        # thickness of the upper (thin) section (Y)
T_LOW = 16.8      # thickness of the lower (thick) section (Y)
Z_SLOPE_TOP = 65.2    # back slope starts (top)
Z_SLOPE_BOT = 46.1    # back slope ends (bottom, sharp-corner position)
R_SLOPE = 8.0         # blend at the bottom of the back slope
R_TOP = T_UP          # top/back round (seen from the side)
R_CORNER = 9.0        # top corner radius seen from the front
R_BACK_V = 1.5        # vertical back edges
R_BACK_B = 0.6        # bottom back edge

WALL = 2.0            # side / bottom wall of the front tray
Z_TRAY_TOP = 75.0     # top of the front tray opening
Y_FLOOR_UP = 8.0      # depth of the shallow (upper) tray floor
Y_FLOOR_LOW = 15.9    # depth of the deep (lower) tray floor

# pocket with the sloped inner back wall
X_POCKET_L = -14.0
Z_POCKET_TOP = 60.0
Y_CEIL = 11.3        # short ceiling at the top of the pocket ...
Z_CEIL = 58.2         # ... ends here, then the inner wall follows the back slope
Z_POCKET_BOT = 46.0   # sharp-corner position of the bottom of the inner slope
R_CEIL = 3.0          # blend ceiling -> inner slope
R_FLOOR = 10.0        # blend inner slope -> deep floor
Z_VALLEY = 43.6       # the ramp meets the deep floor here
R_VALLEY = 1.5        # blend floor -> ramp
R_POCKET_WALL = 1.2   # blend along the left wall of the pocket

# left strip that keeps the thin wall down to the ledge
X_RIDGE = -14.9       # outer recess boundary on the back
Z_STEP_IN = 28.9      # inner step of the tray floor (left strip)
Z_LEDGE = 29.8        # outer ledge at the bottom of the back recess

# latch block + ramp (seen in the front tray)
X_BLK_L = -16.0
X_BLK_R = 1.0
Z_BLK_BOT = 15.2
Z_BLK_TOP = 32.5
Y_RAMP0 = 9.7         # ramp starts here (after a small flat)

# back relief (hollow of the latch, open to the back)
X_REL_L = X_RIDGE
X_REL_R = 0.0
Y_REL = 10.0          # back face of the latch front wall
Z_REL_BOT = 16.5
Z_REL_KNEE = Z_LEDGE  # where the underside of the ramp plate starts
REL_DYDZ = 0.56       # slope of the ramp-plate underside (dY/dZ)
R_RELIEF = 0.7        # rounding of the relief outline on the back

# square window in the latch side wall
WIN_DY = 5.5
WIN_DZ = 4.9
WIN_Y0 = 10.0
WIN_Z0 = 23.8

EPS = 0.01


# ---------------- helpers ----------------
def rounded_poly(wp, pts, radii):
    """Closed polygon on workplane `wp` with corner i rounded by radii[i]."""
    n = len(pts)
    corners = []
    for i in range(n):
        p = pts[i]
        r = radii[i]
        if r <= 0:
            corners.append((p, p, None))
            continue
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        u1 = (a[0] - p[0], a[1] - p[1])
        u2 = (b[0] - p[0], b[1] - p[1])
        l1 = math.hypot(*u1)
        l2 = math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        ang = math.acos(cosang)
        t = r / math.tan(ang / 2)
        p1 = (p[0] + u1[0] * t, p[1] + u1[1] * t)
        p2 = (p[0] + u2[0] * t, p[1] + u2[1] * t)
        bis = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        d = r / math.sin(ang / 2)
        c = (p[0] + bis[0] * d, p[1] + bis[1] * d)
        mid = (c[0] - bis[0] * r, c[1] - bis[1] * r)
        corners.append((p1, p2, mid))
    w = wp.moveTo(*corners[0][1])
    for i in range(1, n + 1):
        p1, p2, mid = corners[i % n]
        w = w.lineTo(*p1)
        if mid is not None:
            w = w.threePointArc(mid, p2)
    return w.close()


# ---------------- outer body ----------------
side = (
    cq.Workplane("YZ", origin=(-W / 2, 0, 0))
    .moveTo(0, 0)
    .lineTo(T_LOW, 0)
    .lineTo(T_LOW, Z_SLOPE_BOT)
    .lineTo(T_UP, Z_SLOPE_TOP)
    .lineTo(T_UP, H - R_TOP)
    .radiusArc((0, H), -R_TOP)
    .close()
    .extrude(W)
)
# blend at the bottom of the back slope
side = side.edges(
    cq.selectors.NearestToPointSelector((0, T_LOW, Z_SLOPE_BOT))
).fillet(R_SLOPE)

front = (
    cq.Workplane("XZ", origin=(0, T_LOW + 1, 0))
    .center(0, H / 2)
    .sketch()
    .rect(W, H)
    .vertices(">Y")
    .fillet(R_CORNER)
    .finalize()
    .extrude(T_LOW + 2)
)

body = side.intersect(front)

# back recess of the left strip (thin wall continues down to the ledge)
recess = cq.Workplane("XY").box(
    X_RIDGE - (-W / 2 - 1), T_LOW - T_UP + 1, H - Z_LEDGE, centered=False
).translate((-W / 2 - 1, T_UP, Z_LEDGE))
body = body.cut(recess)


# soften the back vertical edges (full profile chain on both sides) ...
def _back_chain(shape, x):
    out = []
    for e in shape.edges().vals():
        bb = e.BoundingBox()
        if (
            abs(bb.xmin - x) < 0.01
            and abs(bb.xmax - x) < 0.01
            and bb.ymin > T_UP - 0.1
            and bb.zmin < H - R_TOP - 0.1
            and bb.zmax - bb.zmin > 0.5
        ):
            out.append(e)
    return out


body = body.newObject(_back_chain(body, W / 2) + _back_chain(body, -W / 2)).fillet(R_BACK_V)
# ... and the bottom back edge
body = body.edges(
    cq.selectors.BoxSelector((-W, T_LOW - 0.5, -0.1), (W, T_LOW + 0.1, 0.1))
).edges("|X").fillet(R_BACK_B)

# ---------------- front tray ----------------
tray = cq.Workplane("XY").box(
    W - 2 * WALL, Y_FLOOR_UP + 1, Z_TRAY_TOP - WALL, centered=False
).translate((-W / 2 + WALL, -1, WALL))
body = body.cut(tray)

# deep pocket right of the latch: sloped inner back wall blending into the floor
pocket_r = rounded_poly(
    cq.Workplane("YZ", origin=(X_BLK_R, 0, 0)),
    [
        (Y_FLOOR_UP - EPS, Z_POCKET_TOP),
        (Y_FLOOR_UP, Z_POCKET_TOP),
        (Y_CEIL, Z_CEIL),
        (Y_FLOOR_LOW, Z_POCKET_BOT),
        (Y_FLOOR_LOW, WALL),
        (Y_FLOOR_UP - EPS, WALL),
    ],
    [0, 0, R_CEIL, R_FLOOR, 0, 0],
).extrude(W / 2 - WALL - X_BLK_R)
body = body.cut(pocket_r)

# pocket above the latch: same inner wall, then the ramp down to the latch block
pocket_l = rounded_poly(
    cq.Workplane("YZ", origin=(X_POCKET_L, 0, 0)),
    [
        (Y_FLOOR_UP - EPS, Z_POCKET_TOP),
        (Y_FLOOR_UP, Z_POCKET_TOP),
        (Y_CEIL, Z_CEIL),
        (Y_FLOOR_LOW, Z_POCKET_BOT),
        (Y_FLOOR_LOW, Z_VALLEY),
        (Y_RAMP0, Z_BLK_TOP),
        (Y_FLOOR_UP - EPS, Z_BLK_TOP),
    ],
    [0, 0, R_CEIL, R_FLOOR, R_VALLEY, 0, 0],
).extrude(X_BLK_R - X_POCKET_L)
body = body.cut(pocket_l)

# deep floor below the latch block
below = cq.Workplane("XY").box(
    X_BLK_R - X_BLK_L + EPS, Y_FLOOR_LOW - Y_FLOOR_UP + EPS, Z_BLK_BOT - WALL,
    centered=False,
).translate((X_BLK_L, Y_FLOOR_UP - EPS, WALL))
body = body.cut(below)

# deep lower-left part
lowleft = cq.Workplane("XY").box(
    X_BLK_L - (-W / 2 + WALL) + EPS, Y_FLOOR_LOW - Y_FLOOR_UP + EPS, Z_STEP_IN - WALL,
    centered=False,
).translate((-W / 2 + WALL, Y_FLOOR_UP - EPS, WALL))
body = body.cut(lowleft)

# ---------------- back relief under the ramp plate ----------------
y_far = T_LOW + 2.0
relief = (
    cq.Workplane("YZ", origin=(X_REL_L, 0, 0))
    .polyline(
        [
            (Y_REL, Z_REL_BOT),
            (Y_REL, Z_REL_KNEE),
            (y_far, Z_REL_KNEE + (y_far - Y_REL) / REL_DYDZ),
            (y_far, Z_REL_BOT),
        ]
    )
    .close()
    .extrude(X_REL_R - X_REL_L)
)
body = body.cut(relief)

# square window through the latch side wall
window = cq.Workplane("XY").box(X_BLK_R - X_REL_R + 2, WIN_DY, WIN_DZ, centered=False).translate(
    (X_REL_R - 1, WIN_Y0, WIN_Z0)
)
body = body.cut(window)

# soften the outline of the back relief
relief_edges = [
    body.edges(cq.selectors.NearestToPointSelector(p)).val()
    for p in [
        (X_REL_L, T_LOW, 0.5 * (Z_REL_BOT + Z_REL_KNEE)),
        (0.5 * (X_REL_L + X_REL_R), T_LOW, Z_REL_BOT),
        (X_REL_R, T_LOW, 0.5 * (Z_REL_BOT + Z_REL_KNEE)),
        (0.5 * (X_REL_L + X_REL_R), T_LOW, Z_REL_KNEE + (T_LOW - Y_REL) / REL_DYDZ),
    ]
]
body = body.newObject(relief_edges).fillet(R_RELIEF)

# concave blend along the left wall of the pocket above the latch
pocket_wall_edges = []
for e in body.edges().vals():
    bb = e.BoundingBox()
    if (
        abs(bb.xmin - X_POCKET_L) < 0.01
        and abs(bb.xmax - X_POCKET_L) < 0.01
        and bb.zmax > Z_BLK_TOP + 0.2
        and bb.ymax > Y_FLOOR_UP + 0.3
    ):
        pocket_wall_edges.append(e)
body = body.newObject(pocket_wall_edges).fillet(R_POCKET_WALL)

result = body
